import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
L = 104.0          # overall length (front edge)
W = 31.4           # overall width (Y)
H = 19.8           # overall height (Z)
T = 1.7            # top plate thickness
SLANT = 0.165      # end slant: x-offset per mm of y (back edge shorter)
ZU = H - T         # underside of plate

# -X end notches
Y_M1 = -7.1        # front tab back edge
Y_M2 = 3.7         # back tab front edge
X_M = 14.0         # middle notch depth
X_B1, X_B2, Y_B = 12.2, 22.7, 4.9   # back notch

# +X end U-channel
Y_U1, Y_U2 = -11.7, 11.3
X_U = 89.3
R_U = 2.7

# screw bosses
HOLE_YC = -1.95               # y centre of both screw pairs
HOLES = [(9.15, HOLE_YC - 9.7), (9.15, HOLE_YC + 9.7),      # -X end pair
         (58.05, HOLE_YC - 10.2), (58.05, HOLE_YC + 10.2)]  # middle pair
BOSS_H, BOSS_DT, HOLE_D = 1.6, 3.2, 2.1
BOSS_RF = 1.35               # blend radius at boss base

# slot
SLOT_C = (74.6, 8.0)
SLOT_W, SLOT_L = 5.5, 15.9

# legs
A_T = 2.3                    # -X end wall thickness (front & back)
B_X1, B_Z0 = 15.8, 10.8      # hanging frame end / bottom
B_Y0, B_Y1 = -9.0, Y_B       # hanging frame y extent
C_X0, C_X1, C_REC = 25.6, 36.8, 2.7   # middle legs
D_X0 = 69.6                  # +X front wall start
E_X0 = 77.8                  # +X saddle block start
R_END = 2.8                  # fillet end wall to plate
R_LEG = 2.4                  # fillet legs to plate
R_D = 3.2                    # fillet +X walls to plate
R_AB = 3.2                   # vertical blend between end wall A and frame B

# bore for the tube
BORE_Y, BORE_Z, BORE_R = 0.2, 8.0, 10.7
BORE_X0 = B_X1 + R_LEG        # bore starts just past the frame fillet


def xs(y):
    """x of the -X slanted end at given y"""
    return SLANT * (y + W / 2)


def xe(y):
    """x of the +X slanted end at given y"""
    return L - SLANT * (y + W / 2)


def prism(poly, z0, z1):
    return cq.Workplane("XY").workplane(offset=z0).polyline(poly).close().extrude(z1 - z0)


# ---------------- top plate (trapezoid, ends slanted) ----------------
plate = prism([(xs(-W / 2), -W / 2), (xe(-W / 2), -W / 2),
               (xe(W / 2), W / 2), (xs(W / 2), W / 2)], ZU, H)

body = plate
# -X end front wall A
body = body.union(prism([(xs(-W/2), -W/2), (xs(-W/2) + A_T, -W/2),
                         (xs(Y_M1) + A_T, Y_M1), (xs(Y_M1), Y_M1)], 0, ZU))
# -X end back wall F
body = body.union(prism([(xs(Y_M2), Y_M2), (xs(Y_M2) + A_T, Y_M2),
                         (xs(W/2) + A_T, W/2), (xs(W/2), W/2)], 0, ZU))
# hanging frame B around the middle notch
body = body.union(prism([(xs(B_Y0), B_Y0), (B_X1, B_Y0), (B_X1, B_Y1), (xs(B_Y1), B_Y1)], B_Z0, ZU))
# middle legs (one block, split later by the bore)
body = body.union(prism([(C_X0, -W/2 + C_REC), (C_X1, -W/2 + C_REC),
                         (C_X1, W/2 - C_REC), (C_X0, W/2 - C_REC)], 0, ZU))
# +X front wall D
body = body.union(prism([(D_X0, -W/2), (xe(-W/2), -W/2), (xe(Y_U1), Y_U1), (D_X0, Y_U1)], 0, ZU))
# +X saddle block (later cut by bore and U-channel)
E_X0F = E_X0
body = body.union(prism([(E_X0F, Y_U1), (xe(Y_U1), Y_U1), (xe(W/2), W/2), (E_X0, W/2)], 0, ZU))
body = body.clean()

# ---------------- fillets between hanging parts and plate underside ----------------
solid = body.val()


def find_edge(shape, p, q, z=ZU, tol=0.05):
    for e in shape.Edges():
        a, b = e.startPoint(), e.endPoint()
        if abs(a.z - z) > 1e-3 or abs(b.z - z) > 1e-3:
            continue
        for (u, v) in ((a, b), (b, a)):
            if (abs(u.x - p[0]) < tol and abs(u.y - p[1]) < tol
                    and abs(v.x - q[0]) < tol and abs(v.y - q[1]) < tol):
                return e
    raise ValueError("edge not found %s %s" % (p, q))


end_segs = [
    ((xs(B_Y1) + A_T, B_Y1), (xs(W/2) + A_T, W/2)),     # F inner face
]
leg_segs = [
    ((B_X1, B_Y0), (B_X1, B_Y1)),                        # B +X face
    ((C_X0, -W/2 + C_REC), (C_X1, -W/2 + C_REC)),        # middle legs
    ((C_X1, -W/2 + C_REC), (C_X1, W/2 - C_REC)),
    ((C_X1, W/2 - C_REC), (C_X0, W/2 - C_REC)),
    ((C_X0, W/2 - C_REC), (C_X0, -W/2 + C_REC)),
] 
d_segs = [
    ((D_X0, -W/2), (D_X0, Y_U1)),                        # D start
    ((D_X0, Y_U1), (E_X0F, Y_U1)),                       # D inner face
    ((E_X0, W/2), (E_X0F, Y_U1)),                        # saddle start
]
# vertical concave corner between wall A and the front face of frame B
vert = [e for e in solid.Edges()
        if abs(e.startPoint().x - (xs(B_Y0) + A_T)) < 1e-3 and abs(e.endPoint().x - (xs(B_Y0) + A_T)) < 1e-3
        and abs(e.startPoint().y - B_Y0) < 1e-3 and abs(e.endPoint().y - B_Y0) < 1e-3]
solid = solid.fillet(R_AB, vert)
pocket = [e for e in solid.Edges()
          if abs(e.startPoint().z - ZU) < 1e-3 and abs(e.endPoint().z - ZU) < 1e-3
          and e.Center().x < B_X1 - 0.1 and -W/2 + 0.1 < e.Center().y < B_Y0 + 0.1]
solid = solid.fillet(R_END, pocket + [find_edge(solid, p, q) for p, q in end_segs])
solid = solid.fillet(R_LEG, [find_edge(solid, p, q) for p, q in leg_segs])
solid = solid.fillet(R_D, [find_edge(solid, p, q) for p, q in d_segs])
body = cq.Workplane("XY").add(solid)

# ---------------- notches cut through everything ----------------
body = body.cut(prism([(-5, Y_M1), (X_M, Y_M1), (X_M, Y_M2), (-5, Y_M2)], -1, H + 1))
body = body.cut(prism([(X_B1, Y_B), (X_B2, Y_B), (X_B2, W), (X_B1, W)], -1, H + 1))
uch = (cq.Workplane("XY").workplane(offset=-1)
       .center((X_U + L + 10) / 2, (Y_U1 + Y_U2) / 2)
       .rect(L + 10 - X_U, Y_U2 - Y_U1).extrude(H + 2)
       .edges("|Z and <X").fillet(R_U))
body = body.cut(uch)

# ---------------- bore for the tube ----------------
bore = (cq.Workplane("YZ").workplane(offset=BORE_X0).center(BORE_Y, BORE_Z)
        .circle(BORE_R).extrude(L))
body = body.cut(bore)

# ---------------- screw bosses ----------------
# short cylinder blended into the plate with a large concave fillet ("volcano"), through hole
for hx, hy in HOLES:
    boss = cq.Solid.makeCylinder(BOSS_DT / 2, BOSS_H, cq.Vector(hx, hy, H), cq.Vector(0, 0, 1))
    boss = boss.rotate(cq.Vector(hx, hy, 0), cq.Vector(hx, hy, 1), 135)  # keep seam out of view
    body = body.union(cq.Workplane().add(boss))
solid = body.val()
base_edges = [e for e in solid.Edges()
              if e.geomType() == "CIRCLE" and abs(e.Center().z - H) < 1e-3
              and abs(e.radius() - BOSS_DT / 2) < 1e-3]
solid = solid.fillet(BOSS_RF, base_edges)
body = cq.Workplane("XY").add(solid)
for hx, hy in HOLES:
    body = body.cut(cq.Workplane("XY").workplane(offset=-1).center(hx, hy)
                    .circle(HOLE_D / 2).extrude(H + 5))

# ---------------- slot ----------------
slot = (cq.Workplane("XY").workplane(offset=ZU - 0.05).center(*SLOT_C)
        .slot2D(SLOT_L, SLOT_W).extrude(T + 2))
body = body.cut(slot)

result = body
